import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 200.0          # length along X
W = 112.0          # width along Y
H = 31.0           # height along Z
T_TOP = 3.0        # top plate thickness
T_WALL = 1.7       # side / end wall thickness
R_TOP = 2.4        # outer radius of the top edges (sides and closed -X end)
R_VERT = 1.5       # outer radius of the vertical corners of the closed end
R_VERT_IN = 0.8    # inner radius of those corners
R_BOT = 1.65       # round on the outer bottom edges

# vent grille (diagonal slots in a square field) + 4 countersunk screw holes
HOLE_PITCH = 104.0
HOLE_EDGE = 4.0                      # hole centre distance from the -X end
VENT_CX = -L / 2 + HOLE_EDGE + HOLE_PITCH / 2
VENT_CY = 0.0
VENT_SIZE = 99.0
SLOT_W = 3.0
SLOT_PITCH = 5.55
N_SLOTS = 25
SLOT_SHIFT = -1.1    # offset of the slot pattern across the slots
CSK_HOLE_D = 3.4
CSK_D = 8.4
CSK_ANGLE = 90.0

# screw posts under the +X pair of vent holes
POST_D = 6.6
POST_IN = 5.4        # post axis distance from the outer side face
POST_HOLE_D = 2.6
POST_BOTTOM = 2.5

# +X open end: frame profile
SIDE_FL_W = 6.2      # side flange width (from outer face)
SIDE_GAP = 1.9       # the side flanges stop this far above the bottom edge
DEEP_T = 15.0        # length (along X) of the blocks behind the deep flange
TOP_FL_DEEP = 7.0    # top flange depth near the sides (from the top)
DEEP_W = 26.0        # width of the deep part (from outer face)
R_FRAME_IN = 1.0     # round in the inner corners of the end frame
END_HOLE_D = 4.0
END_HOLE_DEPTH = 10.0   # blind tapped holes in the end blocks
END_HOLE_Z = H - 4.1
END_HOLE_Y = [W / 2 - 8.4, W / 2 - 20.3]

# underside card guides (blocks hanging from the top plate)
GUIDE_X = [34.5, 71.5]        # centre X of the tall guides
TAB_X = [34.5, 66.0]          # centre X of the low tabs
GUIDE_T = 6.0                 # thickness along X
GUIDE_TALL_Y = (3.5, 23.5)    # Y span of the tall block
GUIDE_TALL_D = 10.0           # depth below the top plate underside
GUIDE_LOW_Y = (-31.0, -16.0)  # Y span of the low block
GUIDE_LOW_D = 2.0

# ---------------- main body (outer minus inner) ----------------
outer = cq.Workplane("XY").box(L, W, H, centered=(True, True, False))


def _top_round(e):
    # every top edge except the straight one at the open +X end (left sharp)
    bb = e.BoundingBox()
    if abs(bb.zmin - H) > 1e-6 or abs(bb.zmax - H) > 1e-6:
        return False
    return not (abs(bb.xmin - L / 2) < 1e-6 and abs(bb.xmax - L / 2) < 1e-6)


def _vertical_closed_end(e):
    # the two vertical corners of the closed -X end
    bb = e.BoundingBox()
    return bb.zlen > 1.0 and bb.xlen < 1e-6 and bb.ylen < 1e-6 and bb.xmax < 0


shp = outer.val().fillet(R_TOP, [e for e in outer.edges().vals() if _top_round(e)])
shp = shp.fillet(R_VERT, [e for e in shp.Edges() if _vertical_closed_end(e)])
outer = cq.Workplane("XY").add(shp)
inner = (
    cq.Workplane("XY")
    .box(L - 2 * T_WALL, W - 2 * T_WALL, H - T_TOP + 1.0, centered=(True, True, False))
    .translate((0, 0, -1.0))
    .edges("|Z and <X").fillet(R_VERT_IN)
)
body = outer.cut(inner)

# small round on the outer bottom edges
def _outer_bottom(e):
    bb = e.BoundingBox()
    if abs(bb.zmax) > 1e-3:
        return False
    on_y = abs(abs(bb.ymin) - W / 2) < 1e-3 and abs(abs(bb.ymax) - W / 2) < 1e-3
    on_x = abs(abs(bb.xmin) - L / 2) < 1e-3 and abs(abs(bb.xmax) - L / 2) < 1e-3
    return on_x or on_y


bot_edges = [e for e in body.edges().vals() if _outer_bottom(e)]
body = cq.Workplane("XY").add(body.val().fillet(R_BOT, bot_edges))

# ---------------- +X end: open frame ----------------
x_end = L / 2
yw = W / 2 - T_WALL           # inner face of the side walls
yf = W / 2 - SIDE_FL_W        # inner edge of the side flanges
yd = W / 2 - DEEP_W           # inner end of the deep top flange
half = [
    (yw, -1.0),
    (yw, SIDE_GAP),
    (yf, SIDE_GAP),
    (yf, H - TOP_FL_DEEP),
    (yd, H - TOP_FL_DEEP),
    (yd, H - T_TOP),
]
pts = [(-y, z) for (y, z) in half] + [(y, z) for (y, z) in reversed(half)]
opening = (
    cq.Workplane("YZ", origin=(x_end - T_WALL - 0.5, 0, 0))
    .polyline(pts).close()
    .extrude(T_WALL + 1.0)
)


def _frame_corner(e):
    # opening edges along X at the inner corners of the side / deep flanges
    bb = e.BoundingBox()
    return (bb.ylen < 1e-6 and bb.zlen < 1e-6 and abs(abs(bb.ymin) - yf) < 1e-6
            and abs(bb.zmin - (H - TOP_FL_DEEP)) < 1e-6)


opening = cq.Workplane("XY").add(
    opening.val().fillet(R_FRAME_IN, [e for e in opening.edges().vals() if _frame_corner(e)])
)
body = body.cut(opening)

# thick blocks behind the deep part of the top flange (carry the end holes)
for s in (-1, 1):
    blk = (
        cq.Workplane("XY", origin=(x_end - (DEEP_T + T_WALL) / 2, s * (yd + yw) / 2, H - TOP_FL_DEEP))
        .rect(DEEP_T - T_WALL + 0.2, yw - yd)
        .extrude(TOP_FL_DEEP - T_TOP + 0.2)
    )
    body = body.union(blk)

for yy in END_HOLE_Y:
    for s in (-1, 1):
        hole = (
            cq.Workplane("YZ", origin=(x_end - END_HOLE_DEPTH, 0, 0))
            .center(s * yy, END_HOLE_Z)
            .circle(END_HOLE_D / 2)
            .extrude(END_HOLE_DEPTH + 1.0)
        )
        body = body.cut(hole)

# ---------------- screw posts (D-shaped, joined to the side walls) ----------------
hp = HOLE_PITCH / 2
post_x = VENT_CX + hp
post_h = H - T_TOP - POST_BOTTOM + 0.5
for sy in (-1, 1):
    yc = sy * (W / 2 - POST_IN)
    post = (
        cq.Workplane("XY", origin=(post_x, yc, POST_BOTTOM))
        .circle(POST_D / 2)
        .extrude(post_h)
    )
    web_len = POST_IN - T_WALL + 0.2
    web = (
        cq.Workplane("XY", origin=(post_x, sy * (W / 2 - T_WALL + 0.2 - web_len / 2), POST_BOTTOM))
        .rect(POST_D, web_len)
        .extrude(post_h)
    )
    body = body.union(post).union(web)

# ---------------- underside card guides ----------------
z_under = H - T_TOP
for gx in GUIDE_X:
    tall = (
        cq.Workplane("XY", origin=(gx, (GUIDE_TALL_Y[0] + GUIDE_TALL_Y[1]) / 2, z_under - GUIDE_TALL_D))
        .rect(GUIDE_T, GUIDE_TALL_Y[1] - GUIDE_TALL_Y[0])
        .extrude(GUIDE_TALL_D + 0.5)
    )
    body = body.union(tall)
for tx in TAB_X:
    low = (
        cq.Workplane("XY", origin=(tx, (GUIDE_LOW_Y[0] + GUIDE_LOW_Y[1]) / 2, z_under - GUIDE_LOW_D))
        .rect(GUIDE_T, GUIDE_LOW_Y[1] - GUIDE_LOW_Y[0])
        .extrude(GUIDE_LOW_D + 0.5)
    )
    body = body.union(low)

# ---------------- vent slots ----------------
slot_len = VENT_SIZE * 1.6
slots = None
for i in range(N_SLOTS):
    off = (i - (N_SLOTS - 1) / 2) * SLOT_PITCH + SLOT_SHIFT
    # offset along (1,1)/sqrt2, slot runs along (1,-1)
    cx = VENT_CX + off / math.sqrt(2)
    cy = VENT_CY + off / math.sqrt(2)
    s = (
        cq.Workplane("XY", origin=(cx, cy, H - T_TOP - 1.0))
        .transformed(rotate=(0, 0, -45))
        .rect(slot_len, SLOT_W)
        .extrude(T_TOP + 2.0)
    )
    slots = s if slots is None else slots.union(s)
field = (
    cq.Workplane("XY", origin=(VENT_CX, VENT_CY, H - T_TOP - 1.0))
    .rect(VENT_SIZE, VENT_SIZE)
    .extrude(T_TOP + 2.0)
)
slots = slots.intersect(field)
body = body.cut(slots)

# countersunk holes at the corners of the vent field (through the posts too)
hole_pts = [(VENT_CX + sx * hp, VENT_CY + sy * hp) for sx in (-1, 1) for sy in (-1, 1)]
body = (
    body.faces(">Z").workplane(origin=(0, 0, H))
    .pushPoints(hole_pts)
    .cskHole(CSK_HOLE_D, CSK_D, CSK_ANGLE, depth=T_TOP + 0.01)
)
for (px, py) in hole_pts[2:]:
    body = body.cut(
        cq.Workplane("XY", origin=(px, py, 0.0)).circle(POST_HOLE_D / 2).extrude(H)
    )

result = body
